import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
AF = 30.0                                  # width across flats
AC = AF / math.cos(math.radians(30))       # width across corners
H = 14.3                                   # nut height
CH_DIA = 1.025 * AF                        # chamfer circle diameter on the end faces
CH_ANGLE = 40.0                            # chamfer angle measured from the end face (deg)
PITCH = 1.4                                # thread pitch
D_MAJOR = 21.4                             # thread major diameter (groove root)
D_MINOR = D_MAJOR - 1.0825 * PITCH         # bore / thread minor diameter
THREAD_ANGLE = 60.0                        # included flank angle
THREAD_PHASE = 0.0                        # rotation of the helix start about Z (deg)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- hex prism ----------------
body = cq.Workplane("XY").polygon(6, AC).extrude(H).translate((0, 0, -H / 2))

# ---------------- double chamfer: intersect with revolved double cone ----------------
r0 = CH_DIA / 2
big = AC / 2 + 2.0
rise = (big - r0) * math.tan(math.radians(CH_ANGLE))
cone = (
    cq.Workplane("XZ")
    .polyline([
        (0, -H / 2),
        (r0, -H / 2),
        (big, -H / 2 + rise),
        (big, H / 2 - rise),
        (r0, H / 2),
        (0, H / 2),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.intersect(cone)


# ---------------- internal thread (helical V-groove) ----------------
def thread_groove(pitch, r_minor, r_major, z_start, length, delta=0.2):
    """Closed solid of a helical 60-degree groove, built from ruled faces
    between four helices (profile corners) plus two planar end caps."""
    t = math.tan(math.radians(THREAD_ANGLE / 2))
    hw_root = pitch / 16.0                      # half width at the major diameter
    hw_in = 0.375 * pitch + delta * t            # half width slightly inside the bore
    r_in = r_minor - delta
    prof = [(r_in, -hw_in), (r_major, -hw_root), (r_major, hw_root), (r_in, hw_in)]
    hel = [
        cq.Wire.makeHelix(pitch, length, r, center=cq.Vector(0, 0, z_start + dz),
                          dir=cq.Vector(0, 0, 1))
        for r, dz in prof
    ]
    faces = []
    n = len(hel)
    for i in range(n):
        faces.append(cq.Face.makeRuledSurface(hel[i].Edges()[0], hel[(i + 1) % n].Edges()[0]))
    for use_end in (False, True):
        pts = [h.endPoint() if use_end else h.startPoint() for h in hel]
        faces.append(cq.Face.makeFromWires(cq.Wire.makePolygon(pts, close=True)))
    return cq.Solid.makeSolid(cq.Shell.makeShell(faces)).fix()


def ring_grooves(pitch, r_minor, r_major, delta=0.2):
    """Fallback: stack of revolved annular V-grooves (same profile, no helix)."""
    t = math.tan(math.radians(THREAD_ANGLE / 2))
    hw_root = pitch / 16.0
    hw_in = 0.375 * pitch + delta * t
    r_in = r_minor - delta
    n = int(math.ceil(H / pitch)) + 2
    solid = None
    for k in range(-n // 2 - 1, n // 2 + 2):
        zc = k * pitch
        ring = (
            cq.Workplane("XZ")
            .polyline([(r_in, zc - hw_in), (r_major, zc - hw_root),
                       (r_major, zc + hw_root), (r_in, zc + hw_in)])
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
        )
        solid = ring if solid is None else solid.union(ring)
    return solid


z0 = -H / 2 - 2 * PITCH
vol_before = body.val().Volume()
try:
    groove = thread_groove(PITCH, D_MINOR / 2, D_MAJOR / 2, z0, H + 4 * PITCH)
    groove = groove.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), THREAD_PHASE)
    threaded = body.cut(cq.Workplane("XY").add(groove))
    ok = threaded.val().isValid() and threaded.val().Volume() < vol_before - 1.0
except Exception:
    ok = False
if not ok:
    threaded = body.cut(ring_grooves(PITCH, D_MINOR / 2, D_MAJOR / 2))
body = threaded

# ---------------- bore (minor diameter) ----------------
bore = cq.Workplane("XY").circle(D_MINOR / 2).extrude(H + 4).translate((0, 0, -H / 2 - 2))
body = body.cut(bore)

result = body
